import math
import cadquery as cq

# ---------------- Driving dimensions (mm) ----------------
n = 8                 # holes per row / column (square grid)
pitch = 10.0          # hole grid pitch
margin = 3.875        # plate edge to first hole centre
thick = 7.75          # plate thickness
cb_dia = 6.2          # counterbore diameter (top side)
cb_depth = 4.0        # counterbore depth
thru_dia = 3.8        # through-hole diameter
small_dia = 1.7       # small locating-hole diameter (4 off, near corners)
seam_angle = -135.0   # orientation of cylinder seams (cosmetic, deg about Z)

width = (n - 1) * pitch + 2 * margin

# ---------------- Base plate ----------------
plate = cq.Workplane("XY").rect(width, width).extrude(thick)

# ---------------- Hole positions ----------------
off = (n - 1) * pitch / 2.0
grid_pts = [(-off + i * pitch, -off + j * pitch) for i in range(n) for j in range(n)]

# small locating holes: centred diagonally between each corner hole and its
# inner diagonal neighbour
s = off - pitch / 2.0
small_pts = [(-s, -s), (s, -s), (-s, s), (s, s)]

xdir = (math.cos(math.radians(seam_angle)), math.sin(math.radians(seam_angle)), 0.0)


def cutters(points, dia, z0, height):
    """Vertical cylindrical cutting tools at the given XY points."""
    solids = []
    for (x, y) in points:
        pl = cq.Plane(origin=(x, y, z0), xDir=xdir, normal=(0, 0, 1))
        solids.append(cq.Workplane(pl).circle(dia / 2.0).extrude(height).val())
    return cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])


cbores = cutters(grid_pts, cb_dia, thick - cb_depth, cb_depth + 1.0)
thrus = cutters(grid_pts, thru_dia, -1.0, thick + 2.0)
smalls = cutters(small_pts, small_dia, -1.0, thick + 2.0)

result = plate.cut(cbores).cut(thrus).cut(smalls)

VIEW = {"azimuth": 45, "elevation": 26}
